import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BALL_D = 20.0          # ball diameter
HOLE_D = 8.0           # through bore diameter
THREAD_MAJOR_D = 18.9  # thread major diameter
THREAD_DEPTH = 1.28    # radial thread depth
PITCH = 3.0            # thread pitch (single start, right hand)
THREAD_PHASE_Z = -8.28 # height at which a thread crest centre sits on +X
THREAD_TOP_Z = -6.0    # top face of threaded shank (ball centre at z=0)
THREAD_LEN = 10.0      # length of threaded shank
CREST_FLAT = 0.95      # axial width of crest flat
ROOT_FLAT = 0.5        # axial width of root flat
SEAM_ANGLE = 90.0      # polar angle of the ball's seam meridian (cosmetic)
BORE_SEAM_ANGLE = 45.0 # polar angle of the bore's seam line (cosmetic)

R = BALL_D / 2.0
r_maj = THREAD_MAJOR_D / 2.0
r_min = r_maj - THREAD_DEPTH
z_top = THREAD_TOP_Z
z_bot = THREAD_TOP_Z - THREAD_LEN
FUZZ = 1e-4

# ---------------- ball ----------------
ball = (cq.Workplane("XY").sphere(R)
        .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE))

# ---------------- threaded shank core ----------------
core = (cq.Workplane("XY").workplane(offset=z_bot)
        .circle(r_min).extrude(THREAD_LEN)
        .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE))

# ---------------- helical thread tooth ----------------
tooth_root_w = PITCH - ROOT_FLAT
embed = 0.3
# start the helix an integer number of pitches below the phase height
n_below = int((THREAD_PHASE_Z - z_bot) / PITCH) + 2
z0 = THREAD_PHASE_Z - n_below * PITCH
helix_h = (z_top - z0) + 2 * PITCH
helix = cq.Wire.makeHelix(pitch=PITCH, height=helix_h, radius=r_min - embed,
                          center=cq.Vector(0, 0, z0))
pts = [
    (r_min - embed, z0 - tooth_root_w / 2),
    (r_min, z0 - tooth_root_w / 2),
    (r_maj, z0 - CREST_FLAT / 2),
    (r_maj, z0 + CREST_FLAT / 2),
    (r_min, z0 + tooth_root_w / 2),
    (r_min - embed, z0 + tooth_root_w / 2),
]
thread = (cq.Workplane("XZ").polyline(pts).close()
          .sweep(cq.Workplane("XY").add(helix), isFrenet=True))

# trim thread to shank length
trim = (cq.Workplane("XY").workplane(offset=z_bot)
        .circle(r_maj + 1.0).extrude(THREAD_LEN))
thread = thread.intersect(trim)

shank = core.union(thread, tol=FUZZ)
# guard: the fused shank must contain the whole core (fall back to a
# non-fuzzy fuse without cleaning if the fuzzy fuse ever misbehaves)
if shank.val().Volume() < core.val().Volume():
    shank = core.union(thread, clean=False)
body = ball.union(shank, tol=FUZZ)

# ---------------- through bore ----------------
bore = (cq.Workplane("XY").workplane(offset=z_bot - 1)
        .circle(HOLE_D / 2).extrude(R - z_bot + 2)
        .rotate((0, 0, 0), (0, 0, 1), BORE_SEAM_ANGLE))
result = body.cut(bore, tol=FUZZ)

VIEW = {"azimuth": 45, "elevation": 26}
